import cadquery as cq

# ---------------- driving dimensions (mm) ----------------
W = 131.5          # outer width  (X)
D = 100.0          # outer depth  (Y)
H = 19.0           # outer height (Z)
T_WALL = 3.0       # wall thickness
T_FLOOR = 2.8      # floor thickness
R_CORNER = 2.5     # outer vertical corner radius
R_BOTTOM = 1.5     # outer bottom edge fillet
R_INNER = 0.8      # inner floor/wall fillet

# corner bosses
BOSS_INSET = 10.2  # boss centre from outer edges
BOSS_D = 9.0
BOSS_H = 2.85      # above floor
BOSS_FILLET = 1.0
HOLE_D = 3.5
CBORE_D = 6.5      # counterbore on the underside
CBORE_DEPTH = 2.5

# front wall (-Y) cut-out with two tabs
FRONT_CUT_X0 = -46.85
FRONT_CUT_X1 = 48.3
FRONT_CUT_Z = 8.0           # bottom of the cut-out
TABS = [(-34.6, -18.3), (18.4, 36.0)]
TAB_TOP = 14.05
TAB_HOLE_D = 2.2
TAB_HOLE_Z = 8.4
TAB_HOLES_X = [-28.0, -21.8, 26.8]
R_CUT_EDGE = 0.5            # small round on the outer edges of the cut-out

# back wall (+Y) openings
BIG_OPEN_X = (-48.3, -27.9)
BIG_OPEN_TOP = 7.9
WINDOW_X = (-3.35, 8.8)
WINDOW_Z = (7.75, 13.35)
BACK_HOLE_X = -13.0
BACK_HOLE_Z = 10.4
BACK_HOLE_D = 3.0

# underside label recess
LABEL_W = 48.5
LABEL_D = 40.0
LABEL_DEPTH = 0.5


def box(x0, x1, y0, y1, z0, z1):
    return (cq.Workplane("XY")
            .box(x1 - x0, y1 - y0, z1 - z0, centered=False)
            .translate((x0, y0, z0)))


# ---------------- outer shell ----------------
body = (cq.Workplane("XY")
        .box(W, D, H, centered=(True, True, False))
        .edges("|Z").fillet(R_CORNER)
        .faces("<Z").edges().fillet(R_BOTTOM))

# cavity with filleted floor edges
cavity = (cq.Workplane("XY")
          .box(W - 2 * T_WALL, D - 2 * T_WALL, H, centered=(True, True, False))
          .translate((0, 0, T_FLOOR))
          .faces("<Z").edges().fillet(R_INNER))
body = body.cut(cavity)

# ---------------- corner bosses ----------------
bx = W / 2 - BOSS_INSET
by = D / 2 - BOSS_INSET
boss_pts = [(sx * bx, sy * by) for sx in (-1, 1) for sy in (-1, 1)]

R = BOSS_D / 2
rf = BOSS_FILLET
# revolve profile (in XZ plane, X = radius) with a concave base fillet
boss_prof = (cq.Workplane("XZ")
             .moveTo(0, -0.5)
             .lineTo(R + rf, -0.5)
             .lineTo(R + rf, 0)
             .radiusArc((R, rf), rf)
             .lineTo(R, BOSS_H)
             .lineTo(0, BOSS_H)
             .close()
             .revolve(360, (0, 0, 0), (0, 1, 0)))
for (px, py) in boss_pts:
    body = body.union(boss_prof.translate((px, py, T_FLOOR)))

# through holes + underside counterbores
for (px, py) in boss_pts:
    hole = (cq.Workplane("XY").circle(HOLE_D / 2).extrude(H)
            .translate((px, py, -1)))
    cb = (cq.Workplane("XY").circle(CBORE_D / 2).extrude(CBORE_DEPTH + 1)
          .translate((px, py, -1)))
    body = body.cut(hole).cut(cb)

# ---------------- front wall cut-out with tabs ----------------
yf0 = -D / 2 - 1
yf1 = -D / 2 + T_WALL + 1
front_cut = box(FRONT_CUT_X0, FRONT_CUT_X1, yf0, yf1, FRONT_CUT_Z, H + 1)
for (tx0, tx1) in TABS:
    front_cut = front_cut.cut(box(tx0, tx1, yf0 - 1, yf1 + 1, FRONT_CUT_Z - 1, TAB_TOP))
body = body.cut(front_cut)

# soften the outer edges of the cut-out (vertical sides and lowered sills,
# the tab tops stay sharp)
sel = cq.selectors.BoxSelector((FRONT_CUT_X0 - 0.1, -D / 2 - 0.1, FRONT_CUT_Z - 0.1),
                               (FRONT_CUT_X1 + 0.1, -D / 2 + 0.1, H + 0.1))
cut_edges = [e for e in body.edges(sel).vals()
             if abs(e.Center().z - TAB_TOP) > 0.01]
body = cq.Workplane("XY").add(body.val().fillet(R_CUT_EDGE, cut_edges))

for hx in TAB_HOLES_X:
    h = (cq.Workplane("XZ").center(hx, TAB_HOLE_Z).circle(TAB_HOLE_D / 2)
         .extrude(-(T_WALL + 2)).translate((0, -D / 2 - 1, 0)))
    body = body.cut(h)

# ---------------- back wall openings ----------------
yb0 = D / 2 - T_WALL - 1.5
yb1 = D / 2 + 1
body = body.cut(box(BIG_OPEN_X[0], BIG_OPEN_X[1], yb0, yb1, T_FLOOR, BIG_OPEN_TOP))
body = body.cut(box(WINDOW_X[0], WINDOW_X[1], D / 2 - T_WALL - 1, yb1,
                    WINDOW_Z[0], WINDOW_Z[1]))
bh = (cq.Workplane("XZ").center(BACK_HOLE_X, BACK_HOLE_Z).circle(BACK_HOLE_D / 2)
      .extrude(-(T_WALL + 2)).translate((0, D / 2 - T_WALL - 1, 0)))
body = body.cut(bh)

# ---------------- underside label recess ----------------
body = body.cut(box(-LABEL_W / 2, LABEL_W / 2, -LABEL_D / 2, LABEL_D / 2,
                    -1, LABEL_DEPTH))

result = body

VIEW = {"azimuth": 45, "elevation": 26}
